import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
# Blade (dozer blade shell) - profile in XZ, extruded along Y
BL_LEN = 256.0          # length along Y
BL_BACK = 86.0          # x of flat back face
BL_SPIKE = (56.9, 104.8)  # top tip of the blade edge
COVE_R = 29.0           # radius of concave top cove
BL_WALL = 3.5           # shell wall thickness
BL_RIB_T = 3.0          # transverse rib thickness
BL_N_CELLS = 6          # compartments under the blade
END_A = 18.0            # lowered end section at -Y end
END_B = 13.0            # lowered end section at +Y end
END_DROP = 3.6          # end sections meet the back face this much lower
TAB_W = 10.0            # corner tab size
TAB_H = 58.0

# Base plate / motor mount
PL_X0, PL_X1 = 119.0, 230.5
PL_Y0, PL_Y1 = 33.7, 158.2
PL_T = 10.0
PL_STEP = 3.0           # height of relieved bottom step
PL_STEP_IN = 1.2        # inset of the bottom step
LEDGE_DY = 5.5          # bore ledge in the plate starts this far behind the cup centre
GROOVE_Z = 25.0         # height of split groove in the cup
TAIL_R = 9.0            # rounding of the clamp tail top (+Y end)
TAIL_SIDE_R = 16.0      # rounding of the clamp tail top (-X side)
BOSS_Y0 = 146.0         # clamp screw boss (sloped wedge at the back of the tail)
BOSS_X0, BOSS_X1 = 143.0, 178.0
BOSS_Z_LOW = 29.0
BOSS_HOLE = (151.8, 19.0)   # (y, z) of the clamp screw hole through the wedge
PL_R = 8.0
PL_HOLE_D = 4.5
PL_HOLE_X = (132.0, 222.0)
PL_HOLE_Y = (149.0, 41.7)
LOBE_Y = 95.9           # side lobes of the plate cut-out
LOBE_SPAN = 64.9        # centre distance of the two lobes
LOBE_R = 7.9
SLOT_W = 35.6           # rectangular cut-out toward the side block
TAIL_END_X = 186.0      # clamp tail outline (right side arc)
TAIL_MID = (201.0, 138.0)
CLAMP_HOLE = (183.0, 134.7)
WIN_X0, WIN_Z0, WIN_W, WIN_H = 125.5, 10.0, 16.0, 19.0   # window in side block
CB_HOLE = (174.4, 20.0)  # counterbored hole in side block (x, z)
CUP_C = (181.0, 110.5)
CUP_RI = 21.2
CUP_RO = 23.6
CUP_H = 39.4
CUP_TOP_FR = 3.0        # rounding of the cup top edge
BOSS_SLOPE = (CUP_H - BOSS_Z_LOW) / (BOSS_X1 - BOSS_X0)   # wedge top meets the cup top
BLK_X1 = 188.0
BLK_Y1 = 56.2
BLK_H = 32.0
BLK_WALL = 3.0          # wall of the hollow side block
SCREW_Z = 20.0          # slotted screw head recessed in the block's +X face
SCREW_HOLE_R = 6.0
SCREW_DEPTH = 2.2
BLK_CAV_X1 = BLK_X1 - BLK_WALL   # hollow interior of the block ends here

# Gears
GEAR_CENTERS = [(156.3, 206.5), (209.9, 206.5)]
GEAR_RT = 20.6          # tip radius
GEAR_RR = 19.3          # root radius
GEAR_N = 36
GEAR_HUB_H = 15.0
GEAR_TOP = 31.0
GEAR_PIN_R = 7.5
GEAR_PIN_TOP = 43.0

# Pulley / bushing
PUL_C = (104.8, 205.0)
PUL_FLANGE_R, PUL_FLANGE_T = 13.0, 3.0
PUL_BODY_R, PUL_BODY_TOP = 7.8, 16.0
PUL_PIN_R, PUL_PIN_TOP = 4.8, 21.0

# Lever
LEV_Y0, LEV_Y1 = 240.4, 252.9
LEV_X0 = 111.5
LEV_PIN = (187.1, 264.9)
LEV_PIN_R = 7.4
LEV_PIN_TOP = 25.6
LEV_Z0, LEV_Z1 = 9.0, 26.0   # lever bar bottom / top
LEV_X1 = 236.0
LEV_BLK_H = 20.0
LEV_FLOOR = 8.6          # thickness of the lobe floor under the pin


# ---------------------------------------------------------------------------
# Blade
# ---------------------------------------------------------------------------
def blade_profile():
    sx, sz = BL_SPIKE
    cx, cz = BL_BACK, sz
    a = math.radians(45)
    mid = (cx - COVE_R * math.cos(a), cz - COVE_R * math.sin(a))
    w = (
        cq.Workplane("XZ")
        .moveTo(0, 0)
        .lineTo(BL_BACK, 0)
        .lineTo(BL_BACK, cz - COVE_R)
        .threePointArc(mid, (sx, sz))
        .spline(front_curve_pts(), includeCurrent=True)
        .threePointArc((0.6, 10.6), (0, 9.0))
        .close()
    )
    return w


def front_curve_pts():
    return [(52.6, 92.9), (48.9, 74.9), (44.0, 61.9), (37.5, 48.8), (29.3, 36.5),
            (21.1, 27.5), (13.0, 20.2), (3.1, 12.0)]


def inner_profile_wire():
    """Inner cavity outline (open at the bottom), offset inward by BL_WALL."""
    sx, sz = BL_SPIKE
    outer = cq.Edge.makeSpline([cq.Vector(sx, 0, sz)] +
                               [cq.Vector(p[0], 0, p[1]) for p in front_curve_pts()])
    pts = []
    for t in (0.12, 0.3, 0.5, 0.7, 0.88, 0.95):
        p = outer.positionAt(t)
        tg = outer.tangentAt(t)
        n = cq.Vector(-tg.z, 0, tg.x).normalized()   # points into the material
        q = p + n * BL_WALL
        pts.append((q.x, q.z))
    cx, cz = BL_BACK, sz
    r2 = COVE_R + BL_WALL
    xb = BL_BACK - BL_WALL
    zb = cz - math.sqrt(r2 ** 2 - (cx - xb) ** 2)
    a0 = math.atan2(zb - cz, xb - cx)
    # the cove arc meets the front curve near the top; end the arc at pts[0]
    p0 = pts[0]
    a1 = math.atan2(p0[1] - cz, p0[0] - cx)
    am = 0.5 * (a0 + a1)
    w = (cq.Workplane("XZ")
         .moveTo(xb, -1.0)
         .lineTo(xb, zb)
         .threePointArc((cx + r2 * math.cos(am), cz + r2 * math.sin(am)),
                        (cx + r2 * math.cos(a1), cz + r2 * math.sin(a1)))
         .spline(pts[1:], includeCurrent=True)
         .lineTo(pts[-1][0] + 1.0, -1.0)
         .close())
    return w.wires().val()


def blade():
    body = blade_profile().extrude(-BL_LEN)

    sx, sz = BL_SPIKE

    def end_cut():
        # region above the lowered cove of the end sections
        return (
            cq.Workplane("XZ")
            .moveTo(52.6, 92.9)
            .threePointArc((64.0, 79.5), (BL_BACK, sz - COVE_R - END_DROP))
            .lineTo(BL_BACK + 5, sz - COVE_R - END_DROP)
            .lineTo(BL_BACK + 5, sz + 10)
            .lineTo(40, sz + 10)
            .lineTo(40, 92.9)
            .close()
        )

    # hollow underside: inner profile offset from the outer one by the wall,
    # split into compartments by transverse ribs
    inner = inner_profile_wire()
    cell_len = (BL_LEN - 2 * BL_WALL - (BL_N_CELLS - 1) * BL_RIB_T) / BL_N_CELLS
    y = BL_WALL
    f = cq.Face.makeFromWires(inner)
    # keep material under the lowered end sections and around the corner socket
    keep_a = end_cut().extrude(-END_A - BL_WALL).translate((0, 0, -BL_WALL))
    keep_b = end_cut().extrude(-END_B - BL_WALL).translate(
        (0, BL_LEN - END_B - BL_WALL, -BL_WALL))
    keep_c = cq.Workplane("XY").box(TAB_W + 8, TAB_W + BL_WALL, 200, centered=False) \
        .translate((BL_BACK - TAB_W - 8, -1, -50))
    for i in range(BL_N_CELLS):
        cav = cq.Workplane().add(
            cq.Solid.extrudeLinear(f, cq.Vector(0, cell_len, 0)).translate((0, y, 0)))
        if i == 0:
            cav = cav.cut(keep_a).cut(keep_c)
        if i == BL_N_CELLS - 1:
            cav = cav.cut(keep_b)
        body = body.cut(cav)
        y += cell_len + BL_RIB_T

    # lowered top at both end sections
    body = body.cut(end_cut().extrude(-END_A))
    body = body.cut(end_cut().extrude(-END_B).translate((0, BL_LEN - END_B, 0)))

    # slots through the back wall near each end
    for yc in (17.0, BL_LEN - 17.0):
        body = body.cut(cq.Workplane("XY").box(20, 6.5, 12).translate((BL_BACK, yc, 42)))
    # slots through the end walls
    for yc in (0.0, BL_LEN):
        body = body.cut(cq.Workplane("XY").box(6.5, 20, 12).translate((70.0, yc, 41.5)))

    # corner tab at +Y end (lower part slightly recessed)
    body = body.union(cq.Workplane("XY").box(TAB_W, TAB_W, TAB_H - 18.0, centered=False)
                      .translate((BL_BACK - TAB_W, BL_LEN - 0.01, 18.0)))
    body = body.union(cq.Workplane("XY").box(TAB_W - 0.6, TAB_W, 18.01, centered=False)
                      .translate((BL_BACK - TAB_W, BL_LEN - 0.01, 0)))
    # matching socket at -Y end: shallow full-height recess + deep notches
    body = body.cut(cq.Workplane("XY").box(TAB_W, 2.0, 120, centered=False)
                    .translate((BL_BACK - TAB_W, -1, -1)))
    for z0, z1 in ((-1, 18.0), (57.0, 90.0)):
        body = body.cut(cq.Workplane("XY").box(TAB_W, TAB_W - 0.6, z1 - z0, centered=False)
                        .translate((BL_BACK - TAB_W, -1, z0)))
    return body


# ---------------------------------------------------------------------------
# Base plate with cup housing and side block
# ---------------------------------------------------------------------------
def base_plate():
    w = PL_X1 - PL_X0
    h = PL_Y1 - PL_Y0
    cx = (PL_X0 + PL_X1) / 2
    cy = (PL_Y0 + PL_Y1) / 2
    # plate with a small relief step around the bottom edge
    plate = (cq.Workplane("XY").rect(w, h).extrude(PL_T - PL_STEP)
             .edges("|Z").fillet(PL_R).faces(">Z").edges().fillet(1.0)
             .translate((cx, cy, PL_STEP)))
    plate = plate.union(cq.Workplane("XY").rect(w - 2 * PL_STEP_IN, h - 2 * PL_STEP_IN)
                        .extrude(PL_STEP + 0.01).edges("|Z").fillet(PL_R - PL_STEP_IN)
                        .translate((cx, cy, 0)))

    # side block along -Y edge
    blk = (cq.Workplane("XY").box(BLK_X1 - PL_X0, BLK_Y1 - PL_Y0, BLK_H - PL_STEP,
                                  centered=False)
           .translate((PL_X0, PL_Y0, PL_STEP)))
    blk = blk.edges("|Z and <X and <Y").fillet(PL_R - 0.5)
    blk = blk.faces(">Z").edges().fillet(2.5)
    plate = plate.union(blk)
    # hollow interior at the -X end of the block, opened by a window in the -Y face
    plate = plate.cut(cq.Workplane("XY").box(BLK_CAV_X1 - PL_X0 - BLK_WALL,
                                             BLK_Y1 - PL_Y0 - 2 * BLK_WALL,
                                             BLK_H - PL_T - BLK_WALL, centered=False)
                      .translate((PL_X0 + BLK_WALL, PL_Y0 + BLK_WALL, PL_T)))
    plate = plate.cut(cq.Workplane("XY").box(WIN_W, BLK_WALL + 2, WIN_H, centered=False)
                      .translate((WIN_X0, PL_Y0 - 1, WIN_Z0)))
    # counterbored hole in -Y face
    plate = plate.cut(cq.Workplane("XZ").center(*CB_HOLE).circle(2.0).extrude(-30)
                      .translate((0, PL_Y0 - 1, 0)))
    plate = plate.cut(cq.Workplane("XZ").center(*CB_HOLE).circle(3.5).extrude(-2)
                      .translate((0, PL_Y0 - 1, 0)))
    # recessed slotted screw head in the +X face of the block
    yb = (PL_Y0 + BLK_Y1) / 2
    plate = plate.cut(cq.Workplane("YZ").center(yb, SCREW_Z).circle(SCREW_HOLE_R)
                      .extrude(-(1.0 + SCREW_DEPTH)).translate((BLK_X1 + 1, 0, 0)))
    head = (cq.Workplane("YZ").center(yb, SCREW_Z).circle(SCREW_HOLE_R - 1.0)
            .extrude(SCREW_DEPTH - 0.6).translate((BLK_X1 - SCREW_DEPTH - 0.01, 0, 0)))
    head = head.cut(cq.Workplane("XY").box(2.0, 2 * SCREW_HOLE_R, 1.4)
                    .translate((BLK_X1 - 0.6, yb, SCREW_Z)))
    plate = plate.union(head)

    # cup housing: ring + tail toward +Y (clamp)
    ccx, ccy = CUP_C
    tail = (cq.Workplane("XY")
            .moveTo(ccx - CUP_RO, ccy)
            .lineTo(ccx - CUP_RO, PL_Y1 - 1.5)
            .lineTo(TAIL_END_X, PL_Y1 - 1.5)
            .threePointArc(TAIL_MID, (ccx + CUP_RO, ccy))
            .close().extrude(CUP_H))
    # round the top of the tail end (profile in YZ)
    tail_prof = (cq.Workplane("YZ")
                 .moveTo(ccy - 1, 0)
                 .lineTo(PL_Y1 + 1, 0)
                 .lineTo(PL_Y1 + 1, CUP_H - TAIL_R)
                 .threePointArc((PL_Y1 + 1 - TAIL_R * (1 - math.cos(math.pi / 4)),
                                 CUP_H - TAIL_R * (1 - math.sin(math.pi / 4))),
                                (PL_Y1 + 1 - TAIL_R, CUP_H))
                 .lineTo(ccy - 1, CUP_H)
                 .close().extrude(150).translate((100, 0, 0)))
    tail = tail.intersect(tail_prof)
    # large round along the -X top edge of the tail (profile in XZ)
    xl = ccx - CUP_RO
    side_prof = (cq.Workplane("XZ")
                 .moveTo(xl - 1, 0)
                 .lineTo(ccx + CUP_RO + 5, 0)
                 .lineTo(ccx + CUP_RO + 5, CUP_H)
                 .lineTo(xl + TAIL_SIDE_R, CUP_H)
                 .threePointArc((xl + TAIL_SIDE_R * (1 - math.cos(math.pi / 4)),
                                 CUP_H - TAIL_SIDE_R * (1 - math.sin(math.pi / 4))),
                                (xl, CUP_H - TAIL_SIDE_R))
                 .lineTo(xl - 1, CUP_H - TAIL_SIDE_R)
                 .close().extrude(-80).translate((0, ccy, 0)))
    tail = tail.intersect(side_prof)
    # clamp screw boss at the back: a wedge whose top slopes down toward -X
    bx0, bx1 = BOSS_X0, BOSS_X1
    z_hi = BOSS_Z_LOW + (bx1 - bx0) * BOSS_SLOPE
    slope_top = (cq.Workplane("XZ")
                 .polyline([(bx0 - 3, BOSS_Z_LOW - 3 * BOSS_SLOPE), (bx1, z_hi),
                            (bx1, CUP_H + 10), (bx0 - 3, CUP_H + 10)]).close()
                 .extrude(-(PL_Y1 + 2 - BOSS_Y0)).translate((0, BOSS_Y0, 0)))
    tail = tail.cut(slope_top)
    boss = (cq.Workplane("XZ")
            .polyline([(bx0, PL_T - 0.5), (bx1, PL_T - 0.5), (bx1, z_hi),
                       (bx0, BOSS_Z_LOW)]).close()
            .extrude(-(PL_Y1 - 1.5 - BOSS_Y0)).translate((0, BOSS_Y0, 0)))
    boss = boss.intersect(tail_prof)
    cup = (cq.Workplane("XY").center(ccx, ccy).circle(CUP_RO).extrude(CUP_H)
           .union(tail).union(boss))
    # round the outer top edge of the ring and of the tail's curved side
    try:
        cup = cup.faces(">Z").edges("%CIRCLE").fillet(CUP_TOP_FR)
    except Exception:
        try:
            cup = cup.faces(">Z").edges("%CIRCLE").fillet(CUP_TOP_FR * 0.5)
        except Exception:
            pass
    plate = plate.union(cup)
    # bore
    plate = plate.cut(cq.Workplane("XY").center(ccx, ccy).circle(CUP_RI).extrude(CUP_H + 5)
                      .translate((0, 0, PL_T)))
    # split groove around the cup front
    ang0, ang1 = -150.0, 0.0
    def sector(r_out, z0, hgt, a0, a1):
        am = 0.5 * (a0 + a1)
        pts = [(ccx, ccy)]
        for a in (a0, am, a1):
            pts.append((ccx + r_out * math.cos(math.radians(a)),
                        ccy + r_out * math.sin(math.radians(a))))
        return (cq.Workplane("XY").moveTo(*pts[0]).lineTo(*pts[1])
                .threePointArc(pts[2], pts[3]).close().extrude(hgt).translate((0, 0, z0)))
    plate = plate.cut(sector(CUP_RO + 3, GROOVE_Z, 0.8, ang0, ang1))
    # window in lower front (+X side) of the cup
    plate = plate.cut(sector(CUP_RO + 3, PL_T, GROOVE_Z - PL_T, -50.0, 2.0))
    # clamp slit and screw hole at the tail
    hx, hy = CLAMP_HOLE
    plate = plate.cut(cq.Workplane("XY").box(2.0, hy - (ccy + CUP_RI - 3), CUP_H,
                                             centered=False)
                      .translate((hx - 1.0, ccy + CUP_RI - 3, PL_T + 2)))
    plate = plate.cut(cq.Workplane("XY").center(hx, hy).circle(1.6).extrude(60))
    plate = plate.cut(cq.Workplane("YZ").center(BOSS_HOLE[0], BOSS_HOLE[1]).circle(2.2)
                      .extrude(45).translate((140.0, 0, 0)))
    plate = plate.cut(cq.Workplane("YZ").center(BOSS_HOLE[0], BOSS_HOLE[1]).circle(4.3)
                      .extrude(4.5).translate((BOSS_X0 - 3.0, 0, 0)))

    # central cutout in plate: (offset) bore + side lobes + rectangular slot toward -Y
    bore_cut = (cq.Workplane("XY").center(ccx, ccy).circle(CUP_RI).extrude(PL_T + 2)
                .intersect(cq.Workplane("XY").box(2 * CUP_RI + 2, 2 * CUP_RI, PL_T + 2,
                                                  centered=False)
                           .translate((ccx - CUP_RI - 1, ccy + LEDGE_DY - 2 * CUP_RI, 0))))
    cut = (bore_cut
           .union(cq.Workplane("XY").center(ccx, LOBE_Y)
                  .slot2D(LOBE_SPAN + 2 * LOBE_R, 2 * LOBE_R).extrude(PL_T + 2))
           .union(cq.Workplane("XY").box(SLOT_W, ccy - BLK_Y1, PL_T + 2, centered=False)
                  .translate((ccx - SLOT_W / 2, BLK_Y1 + 0.01, 0)))
           .translate((0, 0, -1)))
    plate = plate.cut(cut)

    # corner holes
    pts = [(x, y) for x in PL_HOLE_X for y in PL_HOLE_Y]
    plate = plate.cut(cq.Workplane("XY").pushPoints(pts).circle(PL_HOLE_D / 2)
                      .extrude(60).translate((0, 0, -1)))
    return plate


# ---------------------------------------------------------------------------
# Spur gear with hub and pin
# ---------------------------------------------------------------------------
def gear_body():
    hub = cq.Workplane("XY").circle(GEAR_RR - 0.4).extrude(GEAR_HUB_H + 0.01)
    pitch = 2 * math.pi / GEAR_N
    tw_root = GEAR_RR * pitch * 0.62
    tw_tip = GEAR_RT * pitch * 0.32
    base = [(GEAR_RR - 0.8, -tw_root / 2), (GEAR_RT, -tw_tip / 2),
            (GEAR_RT, tw_tip / 2), (GEAR_RR - 0.8, tw_root / 2)]
    sk = cq.Sketch().circle(GEAR_RR)
    for i in range(GEAR_N):
        a = i * pitch
        ca, sa = math.cos(a), math.sin(a)
        pts = [(x * ca - y * sa, x * sa + y * ca) for x, y in base]
        sk = sk.polygon(pts + [pts[0]], mode="a")
    ring = (cq.Workplane("XY").placeSketch(sk).extrude(GEAR_TOP - GEAR_HUB_H)
            .translate((0, 0, GEAR_HUB_H)))
    g = hub.union(ring)
    # recessed ring around the pin
    g = g.cut(cq.Workplane("XY").circle(GEAR_PIN_R + 2.0).extrude(1.5)
              .translate((0, 0, GEAR_TOP - 1.5)))
    pin = cq.Workplane("XY").circle(GEAR_PIN_R).extrude(GEAR_PIN_TOP - GEAR_TOP + 1.5) \
        .translate((0, 0, GEAR_TOP - 1.5))
    g = g.union(pin)
    g = g.cut(cq.Workplane("XY").circle(1.5).extrude(8).translate((0, 0, -1)))
    return g


# ---------------------------------------------------------------------------
# Small flanged bushing
# ---------------------------------------------------------------------------
def pulley(cx, cy):
    p = (cq.Workplane("XY").circle(PUL_FLANGE_R).extrude(PUL_FLANGE_T)
         .faces(">Z").workplane().circle(PUL_BODY_R).extrude(PUL_BODY_TOP - PUL_FLANGE_T)
         .faces(">Z").edges().fillet(1.5)
         .faces(">Z").workplane().circle(PUL_PIN_R).extrude(PUL_PIN_TOP - PUL_BODY_TOP))
    p = p.faces(">Z").edges().fillet(1.0)
    return p.translate((cx, cy, 0))


# ---------------------------------------------------------------------------
# Lever arm
# ---------------------------------------------------------------------------
def lever():
    r_end = (LEV_Y1 - LEV_Y0) / 2
    ymid = (LEV_Y0 + LEV_Y1) / 2
    x_a, x_b = 162.3, 214.0
    z0, z1 = LEV_Z0, LEV_Z1
    # straight bar (raised above the ground)
    bar = (cq.Workplane("XY")
           .moveTo(LEV_X0 + r_end, LEV_Y0)
           .lineTo(x_a + 0.5, LEV_Y0)
           .lineTo(x_a + 0.5, LEV_Y1)
           .lineTo(LEV_X0 + r_end, LEV_Y1)
           .threePointArc((LEV_X0, ymid), (LEV_X0 + r_end, LEV_Y0))
           .close().extrude(z1 - z0).translate((0, 0, z0)))
    # curved band around the gear, standing on the ground
    band = (cq.Workplane("XY")
            .moveTo(x_a - 2.1, LEV_Y0)
            .threePointArc((187.0, 232.4), (x_b, LEV_Y0))
            .lineTo(x_b, LEV_Y1)
            .threePointArc((188.0, 242.4), (x_a, LEV_Y1))
            .close().extrude(z1))
    # lower floor (lobe) carrying the pin boss
    px, py = LEV_PIN
    lobe = (cq.Workplane("XY")
            .moveTo(x_a, LEV_Y1)
            .threePointArc((188.0, 242.4), (x_b, LEV_Y1))
            .lineTo(px + LEV_PIN_R * 0.8, py + LEV_PIN_R * 0.6)
            .lineTo(px - LEV_PIN_R * 0.8, py + LEV_PIN_R * 0.6)
            .close().extrude(LEV_FLOOR))
    boss = cq.Workplane("XY").center(px, py).circle(LEV_PIN_R).extrude(LEV_PIN_TOP)
    blk = cq.Workplane("XY").box(LEV_X1 - x_b, LEV_Y1 - LEV_Y0, LEV_BLK_H, centered=False) \
        .translate((x_b, LEV_Y0, 0))
    blk = blk.faces(">X").edges("|Y").fillet(2.0)
    lv = bar.union(band).union(lobe).union(boss).union(blk)
    # holes
    lv = lv.cut(cq.Workplane("XY").center(117.1, ymid).circle(2.2).extrude(40))
    lv = lv.cut(cq.Workplane("XZ").center(224.0, 10.0).circle(3.0).extrude(-8)
                .translate((0, LEV_Y0 - 1, 0)))
    return lv


parts = [blade(), base_plate()]
_g = gear_body()
for c in GEAR_CENTERS:
    parts.append(_g.translate((c[0], c[1], 0)))
parts.append(pulley(*PUL_C))
parts.append(lever())

solids = []
for p in parts:
    solids.extend(p.solids().vals())
comp = cq.Compound.makeCompound(solids)
result = cq.Workplane("XY").add(comp)

VIEW = {"azimuth": 45, "elevation": 26}
